import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Split-keyboard case (Dactyl-style): open bottom at Y=0, curved key plate
# towards +Y, 6x3 main key grid and a raised 3-key thumb cluster.
# Dimensions are taken from the reference front view in "px" and scaled by S.
# ---------------------------------------------------------------------------
S = 0.64            # mm per reference pixel
X0, Z0 = 400.0, 145.0

WALL = 4.0 * S      # side wall thickness
FLANGE = 4.0 * S    # the base rim sticks out this far beyond the walls
FLANGE_H = 8.0 * S  # height of the base rim
PLATE = 6.0 * S     # key plate thickness
HOLE = 21.8 * S     # key switch hole (14 mm)
BIG = 400.0 * S

VIEW = {"azimuth": 45, "elevation": 26}


def X(sx):
    return (sx - X0) * S


def Z(sy):
    return (Z0 - sy) * S


def P(sx, sy):
    return (X(sx), Z(sy))


# --- footprint outline (front view px, clockwise in the picture) -------------
OUTLINE = [
    (271.2, 60.8), (275.5, 50.5), (283.0, 40.0), (291.0, 35.8), (299.0, 37.2),
    (310.0, 44.4), (320.0, 51.4), (330.0, 57.0), (343.0, 61.8), (358.0, 65.4),
    (370.0, 66.8), (377.5, 68.8), (382.0, 74.5), (386.0, 82.0), (391.0, 87.5),
    (399.0, 90.3), (407.0, 90.8), (415.0, 90.6), (424.5, 88.5), (430.5, 82.5),
    (436.0, 77.5), (444.0, 75.7), (460.0, 75.6), (480.0, 75.6), (497.0, 75.7),
    (504.5, 77.8), (508.3, 82.5), (509.4, 90.0), (509.5, 110.0), (509.5, 135.0),
    (509.5, 160.0), (509.3, 182.0), (507.5, 191.5), (501.0, 197.6),
    (490.0, 198.4), (475.0, 198.6), (463.0, 199.2), (454.0, 202.0),
    (444.0, 209.5), (433.0, 216.3), (420.0, 218.4), (405.0, 220.6),
    (392.0, 223.2), (380.0, 223.0), (371.0, 221.6), (362.0, 218.4),
    (345.0, 217.8), (325.0, 217.4), (310.0, 216.4), (302.5, 212.5),
    (299.3, 205.0), (298.2, 190.0), (297.2, 170.0), (296.2, 150.0),
    (295.9, 130.0), (296.2, 112.0), (296.6, 100.0), (295.0, 90.0),
    (288.5, 81.5), (280.0, 75.0), (273.5, 68.5),
]


def outline_wire():
    return cq.Workplane("XZ").spline([P(*p) for p in OUTLINE], periodic=True).close().val()


def outline_prism(offset, y0, y1):
    w = outline_wire()
    if offset:
        w = w.offset2D(offset)[0].toSplines()
    f = cq.Face.makeFromWires(w)
    return cq.Solid.extrudeLinear(f, cq.Vector(0, y1 - y0, 0)).translate((0, y0, 0))


# --- main key columns ---------------------------------------------------------
# Each column is the region below a dished (cylindrical) plate surface, tilted
# about Z (tenting) and cut to its own x-slab; neighbouring columns step.
COLS = [
    # (x_left, x_right, x_centre, z_centre of dish, tilt deg, key rows z)
    # web between the low left wall and column 1 (no keys, upper part only)
    (280.0, 312.0, 304.0, 156.0, -60.0, []),
    (312.0, 341.0, 326.5, 156.0, 20.0, [121.0, 156.3, 190.4]),
    (341.0, 370.0, 355.5, 156.0, 14.0, [121.0, 155.7, 189.0]),
    (370.0, 402.0, 386.0, 160.0, 15.0, [125.0, 160.4, 194.4]),
    (402.0, 436.0, 419.5, 156.0, 8.0, [121.0, 155.0, 189.0]),
    (436.0, 470.0, 454.5, 136.0, 3.0, [101.8, 135.9, 171.3]),
    (470.0, 520.0, 486.6, 136.0, 0.0, [101.8, 135.9, 171.3]),
]
# plate height (px) at the column centre line, middle of the dish
COL_Y = [27.0, 38.0, 25.1, 14.5, 15.1, 18.8, 19.3]
# column curvature radius (px) of the dished key plate
COL_R = [170.0, 170.0, 170.0, 300.0, 300.0, 300.0, 300.0]
# the dished plate stops rising this far (px) from its centre
COL_CAP = [60.0, 60.0, 60.0, 90.0, 90.0, 90.0, 90.0]
LEFT_H = 18.0      # px, height of the low left wall below the web
WEB_Z = (115.0, 142.0)   # px, the web spans this part of the left side
WEB_TOP = 55.0     # px, highest point of the web


def col_transform(shape, i):
    xl, xr, xc, zc, th, rows = COLS[i]
    return (shape.rotate((0, 0, 0), (0, 0, 1), -th)
            .translate((X(xc), COL_Y[i] * S, Z(zc))))


def slab(xl, xr, y0=-BIG, y1=BIG):
    return cq.Solid.makeBox(X(xr) - X(xl), y1 - y0, 2 * BIG,
                            pnt=cq.Vector(X(xl), y0, -BIG))


def column_region(i, drop):
    """Solid below the dished plate surface of column i (lowered by drop)."""
    xl, xr, xc, zc, th, rows = COLS[i]
    R = COL_R[i] * S
    s_cap = R - math.sqrt(R ** 2 - (COL_CAP[i] * S) ** 2) - drop
    blk = cq.Solid.makeBox(BIG, s_cap + BIG, BIG,
                           pnt=cq.Vector(-BIG / 2, -BIG, -BIG / 2))
    cyl = cq.Solid.makeCylinder(R + drop, BIG,
                                pnt=cq.Vector(-BIG / 2, R, 0),
                                dir=cq.Vector(1, 0, 0))
    reg = col_transform(blk.cut(cyl), i)
    return reg.intersect(slab(xl, xr))


def column_holes(i):
    xl, xr, xc, zc, th, rows = COLS[i]
    cutters = None
    R = COL_R[i] * S
    for zr in rows:
        b = Z(zr) - Z(zc)
        s = R - math.sqrt(R * R - b * b)
        ang = math.degrees(math.atan2(-b, math.sqrt(R * R - b * b)))
        box = cq.Solid.makeBox(HOLE, 6 * PLATE, HOLE,
                               pnt=cq.Vector(-HOLE / 2, -3 * PLATE, -HOLE / 2))
        # switch clip notches on the underside
        notch = cq.Solid.makeBox(HOLE * 0.42, 3 * PLATE, HOLE + 2.0 * S,
                                 pnt=cq.Vector(-HOLE * 0.21, -3.0 * PLATE - PLATE * 0.5, -HOLE / 2 - 1.0 * S))
        c = box.fuse(notch)
        c = c.rotate((0, 0, 0), (1, 0, 0), ang).translate((0, s, b))
        c = col_transform(c, i)
        cutters = c if cutters is None else cutters.fuse(c)
    return cutters


# --- thumb cluster -------------------------------------------------------------
T_N = cq.Vector(-0.392, 0.891, 0.230).normalized()     # plate normal
T_O = cq.Vector(X(349.5), 47.5 * S, Z(86.0))            # point on plate (key 3)
T_D = cq.Vector(55.8, 31.0, -25.0).normalized()        # along the thumb row
THUMB_END = 374.0   # px, open end of the thumb hood
THUMB_EDGE = [(276.0, 74.5), (297.0, 82.0), (320.0, 92.5), (342.0, 100.0), (374.0, 103.5)]
# key centre (front view px) and in-plane rotation of each thumb key
THUMB_KEYS = [((296.0, 62.0), 15.0), ((320.0, 76.0), 2.0), ((349.5, 86.0), -15.0)]
THUMB_ROUND = (361.0, 45.0, 13.0)   # px: x, y of the axis and radius of the hood end


def on_thumb_plane(sx, sy, drop=0.0):
    p = cq.Vector(X(sx), 0, Z(sy))
    o = T_O - T_N * drop
    t = (o - p).dot(T_N) / T_N.y
    return p + cq.Vector(0, t, 0)


def thumb_region(drop):
    """Half space below the (tilted, flat) thumb plate, lowered by drop."""
    pl = cq.Plane(origin=T_O - T_N * drop, xDir=T_D, normal=T_N)
    return cq.Workplane(pl).rect(4 * BIG, 4 * BIG).extrude(-4 * BIG).val()


def thumb_rounder():
    cx, cy, r = THUMB_ROUND
    box = cq.Solid.makeBox(BIG, BIG, 2 * BIG, pnt=cq.Vector(X(cx), cy * S, -BIG))
    cyl = cq.Solid.makeCylinder(r * S, 2 * BIG, pnt=cq.Vector(X(cx), cy * S, -BIG),
                                dir=cq.Vector(0, 0, 1))
    return box.cut(cyl)


def thumb_zone():
    # part of the footprint that belongs to the thumb cluster
    pts = ([P(230, -20), P(THUMB_END, -20)] + [P(*p) for p in THUMB_EDGE[::-1]]
           + [P(230, 62)])
    f = cq.Face.makeFromWires(cq.Wire.makePolygon(
        [cq.Vector(x, -BIG, z) for x, z in pts], close=True))
    return cq.Solid.extrudeLinear(f, cq.Vector(0, 2 * BIG, 0))


def thumb_holes():
    cutters = None
    pl = cq.Plane(origin=T_O, xDir=T_D, normal=T_N)
    for (sx, sy), rot in THUMB_KEYS:
        p = on_thumb_plane(sx, sy)
        box = cq.Solid.makeBox(HOLE, HOLE, 6 * PLATE,
                               pnt=cq.Vector(-HOLE / 2, -HOLE / 2, -3 * PLATE))
        notch = cq.Solid.makeBox(HOLE + 2.0 * S, HOLE * 0.42, 3 * PLATE,
                                 pnt=cq.Vector(-HOLE / 2 - 1.0 * S, -HOLE * 0.21, -3.0 * PLATE - PLATE * 0.5))
        c = box.fuse(notch).rotate((0, 0, 0), (0, 0, 1), rot)
        loc = cq.Location(cq.Plane(origin=p, xDir=pl.xDir, normal=pl.zDir))
        c = c.moved(loc)
        cutters = c if cutters is None else cutters.fuse(c)
    return cutters


def fuse_all(shapes):
    out = shapes[0]
    for s in shapes[1:]:
        out = out.fuse(s)
    return out


def zbox(z_top, z_bot):
    """Everything between two front-view heights (z_top above z_bot in the picture)."""
    return cq.Solid.makeBox(2 * BIG, 2 * BIG, Z(z_top) - Z(z_bot),
                            pnt=cq.Vector(-BIG, -BIG, Z(z_bot)))


def main_region(drop):
    regs = []
    for i in range(len(COLS)):
        r = column_region(i, drop)
        if i == 0:
            # the web only spans part of the left side
            r = r.intersect(zbox(WEB_Z[0], WEB_Z[1])).intersect(
                slab(COLS[0][0], COLS[0][1], -BIG, (WEB_TOP - (PLATE / S if drop else 0.0)) * S))
        regs.append(r)
    # low left wall along the whole left side, open on top where there is no web
    strip = slab(COLS[0][0], COLS[0][1], -BIG, LEFT_H * S if drop == 0 else BIG)
    if drop:
        strip = strip.intersect(zbox(0, WEB_Z[0]).fuse(zbox(WEB_Z[1], 400)))
    regs.append(strip)
    return fuse_all(regs)


# --- build ---------------------------------------------------------------------
# outer solid minus the same construction shrunk by the wall / plate thickness
tz = thumb_zone()
prism_out = outline_prism(0, 0.0, FLANGE_H).fuse(outline_prism(-FLANGE, 0.0, BIG)).clean()
prism_in = outline_prism(-(WALL + FLANGE), -BIG / 4, BIG)

rnd = thumb_rounder()
outer = prism_out.intersect(main_region(0.0).cut(tz).fuse(
    thumb_region(0.0).intersect(tz).cut(rnd)))
inner = prism_in.intersect(main_region(PLATE).cut(tz).fuse(
    thumb_region(PLATE).intersect(tz).cut(rnd)))
body = outer.cut(inner)

# narrow slits between neighbouring key columns: (x, z_top, z_bottom, y_from) px.
# The two deep ones also notch the top and bottom walls.
SLITS = [(341.0, 132.0, 204.0, 4.0), (402.0, 104.0, 212.0, 4.0), (436.0, 112.0, 205.0, 4.0),
         (470.0, 110.0, 188.0, 4.0), (402.0, 40.0, 260.0, 12.8), (436.0, 40.0, 260.0, 12.8)]
SLIT_W = 2.0 * S
cutters = [cq.Solid.makeBox(SLIT_W, BIG, Z(zt) - Z(zb),
                            pnt=cq.Vector(X(sx) - SLIT_W / 2, y0 * S, Z(zb)))
           for sx, zt, zb, y0 in SLITS]

# key switch holes
for i in range(len(COLS)):
    if COLS[i][5]:
        cutters.append(column_holes(i))
cutters.append(thumb_holes())
body = body.cut(*cutters)

# screw bosses on the rim, tied into the nearest wall by a short web
# (boss centre, end of the web inside the wall, boss height) in px
BOSSES = [((308.5, 160.2), (301.5, 160.2), 10.0),
          ((363.9, 205.0), (363.9, 213.0), 10.0),
          ((374.0, 89.0), (379.5, 78.0), 18.0),
          ((439.0, 97.0), (439.0, 82.0), 16.0)]
BOSS_D = 9.5 * S
BOSS_HOLE = 5.0 * S
adds = []
for (bx, bz), (wx, wz), bh in BOSSES:
    h = bh * S
    adds.append(cq.Solid.makeCylinder(BOSS_D / 2, h, pnt=cq.Vector(X(bx), 0, Z(bz)),
                                      dir=cq.Vector(0, 1, 0)))
    a, c = cq.Vector(X(bx), 0, Z(bz)), cq.Vector(X(wx), 0, Z(wz))
    d = (c - a).normalized()
    nrm = cq.Vector(-d.z, 0, d.x) * (BOSS_D / 2)
    f = cq.Face.makeFromWires(cq.Wire.makePolygon([a - nrm, c - nrm, c + nrm, a + nrm], close=True))
    adds.append(cq.Solid.extrudeLinear(f, cq.Vector(0, h, 0)))
body = body.fuse(*adds)

# screw holes (the two rim lobes near the top stay solid), reset button hole
# and cable slot through the bottom wall
PORT_Y = 6.0 * S
cutters = [cq.Solid.makeCylinder(BOSS_HOLE / 2, 40 * S, pnt=cq.Vector(X(bx), -10 * S, Z(bz)),
                                 dir=cq.Vector(0, 1, 0))
           for (bx, bz), _w, bh in BOSSES[:2]]
cutters.append(cq.Solid.makeCylinder(2.2 * S, 30 * S, pnt=cq.Vector(X(313.0), PORT_Y, Z(200.0)),
                                     dir=cq.Vector(0, 0, -1)))
cutters.append(cq.Workplane("XY").workplane(offset=Z(200.0))
               .center(X(338.0), PORT_Y).slot2D(11.0 * S, 3.6 * S).extrude(-30 * S).val())
body = body.cut(*cutters)

result = cq.Workplane("XY").add(body)
